import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OUTER_D = 29.8          # knurled body diameter (diamond knurl left out -> plain cylinder)
HEIGHT = 25.0           # overall height (outer rim of the top face)
EDGE_CH_V = 1.35        # outer edge chamfer, axial length (top and bottom)
EDGE_CH_H = 0.7         # outer edge chamfer, radial length (steep knurl-end chamfer)

DISH_DROP = 0.62        # the top face is a shallow cone, dropping this much toward the bore

SPLINE_TEETH = 28       # serrations in the blind bore
SPLINE_ROOT_D = 15.6    # major (root) diameter of the internal serration
SPLINE_TIP_D = 14.2     # minor (tip) diameter of the internal serration
TOOTH_FRACTION = 0.67   # share of the pitch taken by a V tooth at the root circle
BORE_DEPTH = 16.0       # blind bore depth, measured from the top rim plane
ENTRY_D = 15.86         # entry chamfer diameter (where the dish meets the chamfer)
ENTRY_ANGLE = 4.5       # entry chamfer angle measured from horizontal (deg)

SEAM_ANGLE = 143.0      # where the seams of the revolved faces are placed (hidden side)

VIEW = {"azimuth": 45, "elevation": 26}

R = OUTER_D / 2.0
r_root = SPLINE_ROOT_D / 2.0
r_tip = SPLINE_TIP_D / 2.0
r_entry = ENTRY_D / 2.0
r_top = R - EDGE_CH_H                   # outer edge of the top face
z_entry = HEIGHT - DISH_DROP            # height of the dish at the bore entry

# ---------------- body: revolved profile (chamfered ends, dished top) ----------------
body = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R - EDGE_CH_H, 0)
    .lineTo(R, EDGE_CH_V)
    .lineTo(R, HEIGHT - EDGE_CH_V)
    .lineTo(r_top, HEIGHT)
    .lineTo(r_entry, z_entry)
    .lineTo(0, z_entry)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

# ---------------- serrated blind bore ----------------
pitch = 2.0 * math.pi / SPLINE_TEETH
half_tooth = 0.5 * TOOTH_FRACTION * pitch


def polar(r, a):
    return (r * math.cos(a), r * math.sin(a))


wp = cq.Workplane("XY").workplane(offset=HEIGHT - BORE_DEPTH)
wp = wp.moveTo(*polar(r_root, -half_tooth))
for i in range(SPLINE_TEETH):
    a = i * pitch
    wp = wp.lineTo(*polar(r_tip, a))                       # flank to tooth tip
    wp = wp.lineTo(*polar(r_root, a + half_tooth))         # flank back to root
    a_next = a + pitch - half_tooth
    wp = wp.threePointArc(polar(r_root, 0.5 * (a + half_tooth + a_next)),
                          polar(r_root, a_next))            # groove root arc
bore = wp.close().extrude(BORE_DEPTH + 1.0)

# ---------------- shallow conical entry chamfer (cuts the tooth tops) ----------------
tan_e = math.tan(math.radians(ENTRY_ANGLE))
cone_r0 = r_tip - 0.3                      # a little inside the tooth tips
cone_drop = (r_entry - cone_r0) * tan_e    # depth of the cone below the entry circle
cone_h = cone_drop + 0.5                   # extends a bit above the entry circle
cone = cq.Solid.makeCone(
    cone_r0,
    cone_r0 + cone_h / tan_e,
    cone_h,
    pnt=cq.Vector(0, 0, z_entry - cone_drop),
    dir=cq.Vector(0, 0, 1),
)
# keep the chamfer cone inside the entry circle so it does not touch the dish
cone = cone.intersect(cq.Solid.makeCylinder(r_entry, cone_h + 1.0,
                                            pnt=cq.Vector(0, 0, z_entry - cone_drop - 0.5)))
cone = cone.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)

result = body.cut(bore).cut(cq.Workplane("XY").add(cone))
